import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
COMB_W = 19.0          # comb width (X)
COMB_LEN = 160.0       # comb length (Y)
N_TEETH = 10           # teeth per comb
COMB_H = 24.0          # comb total height incl. base
BASE_T = 4.0           # base strip / plate / lower rail thickness
SLOT_W = 2.5           # card slot width
SLOT_D = 5.7           # card slot depth
TOP_R = 0.8            # fillet on the comb top edges
SLOT_R = 0.6           # rounding of the slot entry edges

INNER_GAP = 91.3       # clear distance between the two combs (X)
PLATE_W = 62.8         # plate width (X), starts under the right comb
PLATE_Y0 = -10.7       # plate start (Y) relative to comb front end
PLATE_LEN = 200.0      # plate length (Y)

RAIL_W = 10.0          # rail width (Y)
RAIL_RIB_W = 3.5       # raised outer rib width
RAIL_H = 10.0          # rib top height
RAIL_X0 = 15.8         # rail start (inside left comb)
RAIL_X1 = 116.5        # rib end (inside right comb)
BAR_X1 = 117.5         # lower rail bar end (under the plate)

BRACE_W = 10.3         # diagonal brace width
BRACE_T = 4.0          # diagonal brace thickness
BRACE_ANGLE = 57.4     # brace angle from +X (deg)
BRACE_LEN = 164.0      # brace length
BRACE_SHIFT = 2.5      # brace offset along its axis from the frame centre

CLIP_T = 4.0           # clip thickness (X)
CLIP_W = 13.0          # clip width (Y)
CLIP_H = 20.6          # clip height from plate bottom
CLIP_SLOT_W = 4.0      # clip U-slot width
CLIP_SLOT_Z = 12.8     # clip U-slot bottom height
CLIP_SEAT_D = 11.0     # spherical seat diameter on the outer face
CLIP_SEAT_DEPTH = 2.5  # spherical seat depth
CLIP_SEAT_Z = 12.5     # spherical seat centre height

PITCH = COMB_LEN / N_TEETH
TOOTH_H = COMB_H - BASE_T
X_RIGHT = COMB_W + INNER_GAP


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def slot_cutter(x0, yc):
    """Card slot through the comb (X) with rounded entry edges."""
    w2 = SLOT_W / 2.0
    zb = COMB_H - SLOT_D
    zt = COMB_H
    r = SLOT_R
    c45 = math.sqrt(0.5)
    prof = (cq.Workplane("YZ").workplane(offset=x0 - 1)
            .moveTo(yc - w2, zb)
            .lineTo(yc - w2, zt - r)
            .threePointArc((yc - w2 - r + r * c45, zt - r + r * c45), (yc - w2 - r, zt))
            .lineTo(yc - w2 - r, zt + 1)
            .lineTo(yc + w2 + r, zt + 1)
            .lineTo(yc + w2 + r, zt)
            .threePointArc((yc + w2 + r - r * c45, zt - r + r * c45), (yc + w2, zt - r))
            .lineTo(yc + w2, zb)
            .close()
            .extrude(COMB_W + 2))
    return prof


def comb(x0):
    """Comb block with rounded top edges and card slots, made of N_TEETH
    separate tooth blocks standing side by side."""
    blk = box(x0, x0 + COMB_W, 0, COMB_LEN, BASE_T, COMB_H)
    blk = blk.faces(">Z").edges().fillet(TOP_R)
    for i in range(N_TEETH):
        blk = blk.cut(slot_cutter(x0, (i + 0.5) * PITCH))
    teeth = []
    for i in range(N_TEETH):
        cell = box(x0 - 1, x0 + COMB_W + 1, i * PITCH, (i + 1) * PITCH, BASE_T - 1, COMB_H + 1)
        teeth.append(blk.intersect(cell))
    return teeth


def rib(y_outer, inward):
    """Raised outer rib of a rail (the flat lower bar belongs to the base frame)."""
    if inward > 0:
        ra, rb = y_outer, y_outer + RAIL_RIB_W
    else:
        ra, rb = y_outer - RAIL_RIB_W, y_outer
    return box(RAIL_X0, RAIL_X1, ra, rb, 0, RAIL_H)


def base_frame():
    """Flat U-shaped base: strip under the left comb plus the two lower rail bars."""
    strip = box(0, COMB_W, 0, COMB_LEN, 0, BASE_T)
    front = box(COMB_W - 1.0, BAR_X1, 0, RAIL_W, 0, BASE_T)
    back = box(COMB_W - 1.0, BAR_X1, COMB_LEN - RAIL_W, COMB_LEN, 0, BASE_T)
    return strip.union(front).union(back)


def brace():
    """Flat diagonal bar across the frame opening (front-left to back-right)."""
    xc = COMB_W + INNER_GAP / 2.0
    yc = COMB_LEN / 2.0
    a = math.radians(BRACE_ANGLE)
    xc += BRACE_SHIFT * math.cos(a)
    yc += BRACE_SHIFT * math.sin(a)
    b = (cq.Workplane("XY").box(BRACE_LEN, BRACE_W, BRACE_T)
         .translate((0, 0, BRACE_T / 2.0))
         .rotate((0, 0, 0), (0, 0, 1), BRACE_ANGLE)
         .translate((xc, yc, 0)))
    return b


def clip(y0):
    """Snap clip on the outer plate edge: rounded-top tab with a spherical seat
    recessed into its outer face and a U-shaped entry slot from the top."""
    x0 = X_RIGHT + PLATE_W - CLIP_T
    r = CLIP_W / 2.0
    zc = CLIP_H - r
    tab = (cq.Workplane("YZ").workplane(offset=x0)
           .moveTo(y0, BASE_T).lineTo(y0 + CLIP_W, BASE_T).lineTo(y0 + CLIP_W, zc)
           .threePointArc((y0 + r, CLIP_H), (y0, zc)).close()
           .extrude(CLIP_T))
    ls = CLIP_H - CLIP_SLOT_Z + 2.0
    slot = (cq.Workplane("YZ").workplane(offset=x0 - 1)
            .center(y0 + r, CLIP_SLOT_Z + ls / 2.0)
            .slot2D(ls, CLIP_SLOT_W, angle=90)
            .extrude(CLIP_T + 2))
    a, h = CLIP_SEAT_D / 2.0, CLIP_SEAT_DEPTH
    rs = (a * a + h * h) / (2.0 * h)
    seat = (cq.Workplane("XY")
            .sphere(rs)
            .translate((x0 + CLIP_T + rs - h, y0 + r, CLIP_SEAT_Z)))
    return tab.cut(slot).cut(seat)


bodies = []
# left comb: teeth standing on the flat base frame
bodies += comb(0.0)
bodies.append(base_frame())
# right comb: teeth standing on the plate
bodies += comb(X_RIGHT)
bodies.append(box(X_RIGHT, X_RIGHT + PLATE_W, PLATE_Y0, PLATE_Y0 + PLATE_LEN, 0, BASE_T))
# raised rail ribs front/back and the diagonal brace
bodies.append(rib(0.0, +1))
bodies.append(rib(COMB_LEN, -1))
bodies.append(brace())
# clips at the outer plate edge
bodies.append(clip(PLATE_Y0))
bodies.append(clip(PLATE_Y0 + PLATE_LEN - CLIP_W))

solids = [b.val() for b in bodies]
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
